import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeWire

# ------------------------------------------------------------------
# Square-mouth to round-throat horn (transition piece)
#   square mouth face at Y = 0, round end face at Y = L (+Y = back)
#   smooth loft: sharp square S -> rounded waist section(s) -> circle D
#   side mid-lines are straight (linear taper S -> D), the corners
#   sweep in on a concave curve and the corner crease fades out into
#   the round end (single smooth lateral face).
#   blind axial hole in the round end face.
# ------------------------------------------------------------------
S = 100.0            # side of the square mouth
L = 80.0             # axial length mouth -> round end
D = 30.0             # diameter of the round end
SQ_POLE = 0.612      # parametrisation of the square sides (inner pole / half side)
# intermediate loft stations: (fraction of L, corner ratio k = c/w, inner-pole ratio g = x1/w)
#   k: 45-deg corner point relative to the side mid-line half width w
#   g: inner pole of each 45-deg span (sets how full the section is)
STATIONS = [
    (0.3666, 0.730, 0.3747),
]
HOLE_D = 10.5        # blind hole in the round end
HOLE_DEPTH = 12.0

a = S / 2.0
r = D / 2.0

W45 = math.cos(math.radians(22.5))      # weight of a 45 deg rational arc span
K_CIRC = 1.0 / math.sqrt(2.0)           # 45 deg point of a circle (relative to radius)
G_CIRC = math.sqrt(2.0) - 1.0           # inner pole of a 45 deg arc (relative to radius)


def section(y, w, c, x1):
    """Closed single-edge section, 8 rational quadratic spans.
    side mid-points (0,+-w),(+-w,0); corners (+-c,+-c) as C0 knots;
    inner poles (+-x1, w) keep the mid-lines tangent-flat.
    Same knots/weights for every section -> one smooth lofted face."""
    def rot(p, k):
        x, z = p
        for _ in range(k):
            x, z = -z, x
        return x, z
    side = [(c, c), (x1, w), (0.0, w), (-x1, w)]
    poles = []
    for k in (2, 3, 0, 1):               # start/seam at the (-c,-c) corner
        poles += [rot(p, k) for p in side]
    poles.append(poles[0])
    n = len(poles)
    P = TColgp_Array1OfPnt(1, n)
    Wt = TColStd_Array1OfReal(1, n)
    for i, (x, z) in enumerate(poles):
        P.SetValue(i + 1, gp_Pnt(x, y, z))
        Wt.SetValue(i + 1, 1.0 if i % 2 == 0 else W45)
    K = TColStd_Array1OfReal(1, 9)
    M = TColStd_Array1OfInteger(1, 9)
    for i in range(9):
        K.SetValue(i + 1, float(i))
        M.SetValue(i + 1, 3 if i in (0, 8) else 2)
    edge = BRepBuilderAPI_MakeEdge(Geom_BSplineCurve(P, Wt, K, M, 2)).Edge()
    return cq.Wire(BRepBuilderAPI_MakeWire(edge).Wire())


def square_section(y, half):
    return section(y, half, half, SQ_POLE * half)


def circle_section(y, radius):
    return section(y, radius, K_CIRC * radius, G_CIRC * radius)


def half_width(t):
    # side mid-lines taper linearly from the square to the round end
    return a + (r - a) * t


wires = [square_section(0.0, a)]
for t, k, g in STATIONS:
    w = half_width(t)
    wires.append(section(t * L, w, k * w, g * w))
wires.append(circle_section(L, r))
horn = cq.Solid.makeLoft(wires, False)

hole = (
    cq.Workplane(cq.Plane(origin=(0, L, 0), xDir=(-1, 0, 0), normal=(0, -1, 0)))
    .circle(HOLE_D / 2.0)
    .extrude(HOLE_DEPTH)
)

result = cq.Workplane("XY").add(horn).cut(hole)

VIEW = {"azimuth": 45, "elevation": 26}
